import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0        # outer width  (X)
D = 92.5         # outer depth  (Y)
H = 214.0        # outer height (Z)
T = 5.8          # wall thickness (top, sides, back)
R_OUT = 3.0      # outer edge rounding (top / back corners)
R_IN = 2.5       # inner corner rounding
R_BOT = 1.5      # small rounding along the bottom edges of the walls

# top slot (through, near the back edge)
SLOT_L = 43.0
SLOT_W = 14.8
SLOT_FROM_BACK = 21.3   # slot centre measured from the outer back face
SLOT_R = 3.0
SLOT_EDGE_R = 1.5

# internal shelf near the bottom
SHELF_TOP = 38.5
SHELF_T = 7.3
OPEN_X = 60.0            # opening size along X
OPEN_Y0 = -34.8          # opening front edge (Y)
OPEN_Y1 = 29.25          # opening back edge (Y)
OPEN_R = 1.5
OPEN_EDGE_R = 3.5
OPEN_EDGE_R_BOT = 3.5
HOLE_D = 6.5
HOLE_X = 38.3
HOLE_YF = -41.5
HOLE_YB = 34.5

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- outer shell (open front, open bottom) ----------------
def round_top_back(wp, r):
    """Round the two top side edges, the top-back edge and the two back vertical edges."""
    bb = wp.val().BoundingBox()
    sel = []
    for e in wp.edges().vals():
        c = e.Center()
        on_top = abs(c.z - bb.zmax) < 1e-6
        on_back = abs(c.y - bb.ymax) < 1e-6
        on_side = abs(c.x - bb.xmin) < 1e-6 or abs(c.x - bb.xmax) < 1e-6
        if (on_top and (on_side or on_back)) or (on_back and on_side):
            sel.append(e)
    return wp.newObject(sel).fillet(r)


outer = cq.Workplane("XY").box(W, D, H, centered=(True, True, False))
outer = round_top_back(outer, R_OUT)

inner_w = W - 2 * T
inner_d = D - T + 10.0
inner_h = H - T + 10.0
inner = (
    cq.Workplane("XY")
    .box(inner_w, inner_d, inner_h, centered=(True, False, False))
    .translate((0, D / 2 - T - inner_d, -10.0))
)
inner = round_top_back(inner, R_IN)

shell = outer.cut(inner)


def bottom_edges(wp):
    """Outer bottom edges of the walls (left, back, right and the back corners)."""
    sel = []
    for e in wp.edges().vals():
        c = e.Center()
        if abs(c.z) > 1e-6 or abs(c.y + D / 2) < 1e-3:
            continue
        outer_side = abs(abs(c.x) - W / 2) < 1e-3
        outer_back = abs(c.y - D / 2) < 1e-3
        outer_corner = abs(c.x) > W / 2 - R_OUT - 1e-3 and c.y > D / 2 - R_OUT - 1e-3
        if outer_side or outer_back or outer_corner:
            sel.append(e)
    return wp.newObject(sel)


shell = bottom_edges(shell).fillet(R_BOT)

# ---------------- slot in the top ----------------
slot_y = D / 2 - SLOT_FROM_BACK
slot = (
    cq.Workplane("XY")
    .workplane(offset=H - T - 1)
    .center(0, slot_y)
    .rect(SLOT_L, SLOT_W)
    .extrude(T + 2)
    .edges("|Z")
    .fillet(SLOT_R)
)
shell = shell.cut(slot)
# rounded (formed-looking) top edge of the slot
shell = shell.edges(
    cq.selectors.BoxSelector(
        (-SLOT_L / 2 - 1, slot_y - SLOT_W / 2 - 1, H - 0.5),
        (SLOT_L / 2 + 1, slot_y + SLOT_W / 2 + 1, H + 0.5),
    )
).fillet(SLOT_EDGE_R)

# ---------------- shelf ----------------
shelf_y0 = -D / 2
shelf_y1 = D / 2 - T
shelf = (
    cq.Workplane("XY")
    .workplane(offset=SHELF_TOP - SHELF_T)
    .center(0, (shelf_y0 + shelf_y1) / 2)
    .rect(inner_w, shelf_y1 - shelf_y0)
    .extrude(SHELF_T)
)
opening = (
    cq.Workplane("XY")
    .workplane(offset=SHELF_TOP - SHELF_T - 1)
    .center(0, (OPEN_Y0 + OPEN_Y1) / 2)
    .rect(OPEN_X, OPEN_Y1 - OPEN_Y0)
    .extrude(SHELF_T + 2)
    .edges("|Z")
    .fillet(OPEN_R)
)
shelf = shelf.cut(opening)
# rounded top edge of the shelf opening
shelf = shelf.edges(
    cq.selectors.BoxSelector(
        (-OPEN_X / 2 - 1, OPEN_Y0 - 1, SHELF_TOP - 0.5),
        (OPEN_X / 2 + 1, OPEN_Y1 + 1, SHELF_TOP + 0.5),
    )
).fillet(OPEN_EDGE_R)
shelf = shelf.edges(
    cq.selectors.BoxSelector(
        (-OPEN_X / 2 - 1, OPEN_Y0 - 1, SHELF_TOP - SHELF_T - 0.5),
        (OPEN_X / 2 + 1, OPEN_Y1 + 1, SHELF_TOP - SHELF_T + 0.5),
    )
).fillet(OPEN_EDGE_R_BOT)
holes = (
    cq.Workplane("XY")
    .workplane(offset=SHELF_TOP - SHELF_T - 1)
    .pushPoints([(-HOLE_X, HOLE_YF), (HOLE_X, HOLE_YF), (-HOLE_X, HOLE_YB), (HOLE_X, HOLE_YB)])
    .circle(HOLE_D / 2)
    .extrude(SHELF_T + 2)
)
shelf = shelf.cut(holes)

result = shell.union(shelf)
